import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 82.4          # outer radius of the spherical sheet (band + disc domes)
SHEET_T = 2.1         # sheet thickness of the band
DISC_R = 30.0         # disc radius
BAND_W = 30.0         # band width (along X)

SHAFT_R = 9.1         # stub shaft radius
SHAFT_END = 121.5     # shaft end position along +/-Y
BORE_D = 6.0          # axial bore through shafts / discs
XHOLE_D = 4.6         # cross hole in the -Y shaft
XHOLE_Y = 106.0       # its distance from centre
XHOLE_DEPTH = 1.5     # visible depth of the cross hole (roll pin inside)

BAR_LEN = 92.0        # flat arm length from shaft axis (towards -X)
BAR_H = 12.0          # arm height (Z)
BAR_T = 3.5           # arm thickness (Y)
BAR_Y = 105.3         # arm position along +Y shaft

PIN_R = 7.5           # centre pin radius
PIN_TOP = -22.5       # pin top height
PIN_STEP_R = 6.0      # reduced top step
PIN_STEP_H = 2.8
NUB_R = 1.3
NUB_H = 2.5
PIN_XHOLE_D = 2.6
PIN_XHOLE_DROP = 2.4   # cross hole centre below the pin body top
COLLAR_R = 9.0
COLLAR_H = 3.5
TAB_W = 6.5
TAB_L = 2.0
SLIT_W = 1.2          # slits in the collar
TAB_T = 1.8

RIVET_D = 4.5         # pin rivet / spigot end seen under the band
RIVET_DEPTH = 0.6

R_IN = R_OUT - SHEET_T
BIG = 400.0

# ---------------- spherical sheet: keyhole discs + U band ----------------
# The whole sheet is one spherical shell (centre at the origin) trimmed to two
# round caps around the Y axis plus a strip of width BAND_W in the lower half.
def ball(r):
    # sphere with its poles on the X axis and its seam in the upper half,
    # so that no seam or pole lies on the trimmed sheet
    return cq.Workplane("XY").sphere(r).rotate((0, 0, 0), (0, 1, 0), -90)

shell = ball(R_OUT).cut(ball(R_IN))
band_box = cq.Workplane("XY").box(BAND_W, BIG, BIG, centered=(True, True, False)).translate((0, 0, -BIG))
cap_cyl = cq.Workplane("XZ").circle(DISC_R).extrude(BIG / 2.0, both=True)
sheet = shell.intersect(band_box.union(cap_cyl))

# ---------------- stub shafts ----------------
def shaft(sign):
    s = (cq.Workplane("XZ").circle(SHAFT_R).extrude(-(SHAFT_END - R_IN - 0.6))
         .translate((0, R_IN + 0.6, 0)))
    if sign < 0:
        s = s.mirror("XZ")
    return s

part = sheet.union(shaft(1)).union(shaft(-1))

# ---------------- flat arm on the +Y shaft ----------------
bar = (cq.Workplane("XY").box(BAR_LEN, BAR_T, BAR_H)
       .translate((-BAR_LEN / 2.0, BAR_Y, 0)))
part = part.union(bar)

# ---------------- centre pin ----------------
pin_base = -R_IN - 1.0
pin_body_h = PIN_TOP - PIN_STEP_H - pin_base
pin = (cq.Workplane("XY").workplane(offset=pin_base).circle(PIN_R).extrude(pin_body_h)
       .faces(">Z").workplane().circle(PIN_STEP_R).extrude(PIN_STEP_H)
       .faces(">Z").workplane().circle(NUB_R).extrude(NUB_H))
collar = cq.Workplane("XY").workplane(offset=pin_base).circle(COLLAR_R).extrude(COLLAR_H + 1.0)
# narrow slits in the collar
for ang in (45, 135, 225, 315):
    notch = (cq.Workplane("XY").box(SLIT_W, 4.0, COLLAR_H + 2)
             .translate((0, COLLAR_R, pin_base + (COLLAR_H + 2) / 2.0 + 0.5))
             .rotate((0, 0, 0), (0, 0, 1), ang))
    collar = collar.cut(notch)
# two small locking tabs (along +/-Y) lying on the band
tabs = (cq.Workplane("XY").box(TAB_W, 2 * (COLLAR_R + TAB_L), TAB_T + 1.0)
        .translate((0, 0, -R_IN + (TAB_T + 1.0) / 2.0 - 1.0)))
pin = pin.union(collar).union(tabs)
# cross hole near pin top (axis along Y)
pin_xh = (cq.Workplane("XZ").circle(PIN_XHOLE_D / 2.0).extrude(20, both=True)
          .translate((0, 0, PIN_TOP - PIN_STEP_H - PIN_XHOLE_DROP)))
pin = pin.cut(pin_xh)
# keep everything that pokes below the band inside the sheet
pin = pin.intersect(ball(R_IN + 0.5))
part = part.union(pin)

# ---------------- holes ----------------
bore = cq.Workplane("XZ").circle(BORE_D / 2.0).extrude(SHAFT_END + 5, both=True)
bore = bore.cut(cq.Workplane("XY").box(BIG, 2 * (R_IN - 3.0), BIG))
part = part.cut(bore)

# cross hole (axis X) in the -Y shaft, plugged by a roll pin: modelled as a
# shallow recess of XHOLE_DEPTH on both sides of the shaft
for x0 in (SHAFT_R - XHOLE_DEPTH, -(SHAFT_R + 2.0)):
    xhole = (cq.Workplane("YZ").circle(XHOLE_D / 2.0).extrude(XHOLE_DEPTH + 2.0)
             .translate((x0, -XHOLE_Y, 0)))
    part = part.cut(xhole)

# riveted end of the pin seen from below the band
rivet = (cq.Workplane("XY").workplane(offset=-R_OUT - 2.0).circle(RIVET_D / 2.0)
         .extrude(2.0 + RIVET_DEPTH))
part = part.cut(rivet)

result = part
